import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
T = 8.2                      # plate thickness

# main outline (XY, Y up).  Edges are given as point + direction lines.
P_UL = (-56.6, 49.2)          # upper-left vertex
UPLEFT_DIR = (-0.404, -1.0)   # edge from UL down to the left lug
LOWLEFT_PT = (-100.3, -65.0)  # point on edge from left lug down to BL
LOWLEFT_DIR = (-0.359, -1.0)
BOTTOM_PT = (-78.0, -102.7)   # bottom edge (BL -> bottom vertex)
BOTTOM_DIR = (33.0, -11.5)
LOWRIGHT_PT = (-6.5, -93.8)   # edge bottom vertex -> kink
LOWRIGHT_DIR = (29.6, 34.2)
RIGHTLOW_PT = (100.0, -5.0)   # edge kink -> right-most vertex
RIGHTLOW_DIR = (1.0, 0.712)
RIGHT_PT = (85.2, 40.0)       # edge right-most vertex -> top lug
RIGHT_DIR = (-1.0, 1.426)

# corner fillet radii
R_BL = 7.0
R_BT = 6.5
R_V = 3.0
R_R = 5.0
R_UL = 1.5

# lugs (mounting ears)
LUG_R = 7.0                  # outer radius of lug
LUG_TOP = (43.6, 111.7)      # top lug centre
LUG_LEFT = (-102.2, -47.3)   # left lug centre
LUG_FILLET_TOP = 5.0         # concave blend radius top lug <-> plate edge
LUG_FILLET_LEFT = 5.0        # concave blend radius left lug <-> plate edge
LUG_CB_D = 11.8              # counterbore diameter in lug (from top)
LUG_CB_DEPTH = 5.5
LUG_HOLE_D = 6.0             # through hole in lug

# plain holes (through, counterbored from below)
HOLE_D = 6.6
HOLE_CB_D = 11.8
HOLE_CB_DEPTH = 4.5
HOLES = [
    (31.8, 103.2),
    (-51.5, 44.2),
    (101.4, 4.7),
    (-76.2, -18.2),
    (-7.55, -42.45),
    (18.5, -54.2),
    (-100.3, -86.9),
    (-32.1, -110.9),
]

# counterbored hole from top
HOLE_TOP_CB = (-6.7, -82.7)
TOP_HOLE_D = 6.0
TOP_CB_D = 12.0
TOP_CB_DEPTH = 5.0

# notch on right edge, open to the bottom
NOTCH_Y0 = 69.0              # notch extent measured in Y along right edge
NOTCH_Y1 = 88.0
NOTCH_DEPTH = 8.0            # perpendicular into the plate
NOTCH_H = 5.8                # height from bottom face


# ---------------------------------------------------------------------------
# 2D helpers
# ---------------------------------------------------------------------------
def v_add(a, b):
    return (a[0] + b[0], a[1] + b[1])


def v_sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def v_mul(a, s):
    return (a[0] * s, a[1] * s)


def v_dot(a, b):
    return a[0] * b[0] + a[1] * b[1]


def v_norm(a):
    l = math.hypot(a[0], a[1])
    return (a[0] / l, a[1] / l)


def left_n(d):
    return (-d[1], d[0])


def right_n(d):
    return (d[1], -d[0])


def line_isect(p1, d1, p2, d2):
    den = d1[0] * d2[1] - d1[1] * d2[0]
    t = ((p2[0] - p1[0]) * d2[1] - (p2[1] - p1[1]) * d2[0]) / den
    return v_add(p1, v_mul(d1, t))


def fillet_ll(l1, l2, r):
    """fillet between two lines (point, unit dir), CCW traversal.
    returns (t1, mid, t2)"""
    p1, d1 = l1
    p2, d2 = l2
    cross = d1[0] * d2[1] - d1[1] * d2[0]
    side = left_n if cross > 0 else right_n
    q1 = v_add(p1, v_mul(side(d1), r))
    q2 = v_add(p2, v_mul(side(d2), r))
    c = line_isect(q1, d1, q2, d2)
    t1 = v_add(p1, v_mul(d1, v_dot(v_sub(c, p1), d1)))
    t2 = v_add(p2, v_mul(d2, v_dot(v_sub(c, p2), d2)))
    x = line_isect(p1, d1, p2, d2)
    m = v_add(c, v_mul(v_norm(v_sub(x, c)), r))
    return t1, m, t2


def fillet_lc(line, c, R, r, incoming):
    """concave fillet between a line and a convex lug circle.
    returns (t_line, mid, t_circ)"""
    p, d = line
    n = right_n(d)
    q0 = v_sub(v_add(p, v_mul(n, r)), c)
    b = v_dot(q0, d)
    disc = b * b - v_dot(q0, q0) + (R + r) ** 2
    s = -b - math.sqrt(disc) if incoming else -b + math.sqrt(disc)
    tl = v_add(p, v_mul(d, s))
    f = v_add(tl, v_mul(n, r))
    tc = v_add(c, v_mul(v_norm(v_sub(f, c)), R))
    chord_mid = v_mul(v_add(tl, tc), 0.5)
    m = v_add(f, v_mul(v_norm(v_sub(chord_mid, f)), r))
    return tl, m, tc


def circle_arc_mid(c, R, a_pt, b_pt):
    """midpoint of CCW arc from a_pt to b_pt around c"""
    a0 = math.atan2(a_pt[1] - c[1], a_pt[0] - c[0])
    a1 = math.atan2(b_pt[1] - c[1], b_pt[0] - c[0])
    while a1 <= a0:
        a1 += 2 * math.pi
    am = 0.5 * (a0 + a1)
    return (c[0] + R * math.cos(am), c[1] + R * math.sin(am))


def tangent_line_from_point(p, c, R):
    """line through p tangent to circle c (circle on left of travel c->p)."""
    v = v_sub(c, p)
    A = v[1]
    B = -v[0]
    base = math.atan2(B, A)
    off = math.acos(R / math.hypot(A, B))
    best = None
    for th in (base + off, base - off):
        d = (math.cos(th), math.sin(th))
        # distance of c from line with d must be +R on the left
        if v_dot(d, v_sub(p, c)) > 0:
            best = d
    tp = v_add(c, v_mul(right_n(best), R))
    return tp, best


# ---------------------------------------------------------------------------
# outline construction
# ---------------------------------------------------------------------------
L_bottom = (BOTTOM_PT, v_norm(BOTTOM_DIR))
L_lowright = (LOWRIGHT_PT, v_norm(LOWRIGHT_DIR))
L_rightlow = (RIGHTLOW_PT, v_norm(RIGHTLOW_DIR))
L_right = (RIGHT_PT, v_norm(RIGHT_DIR))
tp_top, d_up = tangent_line_from_point(P_UL, LUG_TOP, LUG_R)
L_upper = (tp_top, d_up)
L_upleft = (P_UL, v_norm(UPLEFT_DIR))
L_lowleft = (LOWLEFT_PT, v_norm(LOWLEFT_DIR))

# corner blends, lug blends (all computed tangent-exact)
bl1, blm, bl2 = fillet_ll(L_lowleft, L_bottom, R_BL)
bt1, btm, bt2 = fillet_ll(L_bottom, L_lowright, R_BT)
v1, vm, v2 = fillet_ll(L_lowright, L_rightlow, R_V)
r1, rm, r2 = fillet_ll(L_rightlow, L_right, R_R)
tl_in, tm_in, tc_in = fillet_lc(L_right, LUG_TOP, LUG_R, LUG_FILLET_TOP, True)
top_arc_mid = circle_arc_mid(LUG_TOP, LUG_R, tc_in, tp_top)
u1, um, u2 = fillet_ll(L_upper, L_upleft, R_UL)
ll_in, llm_in, lc_in = fillet_lc(L_upleft, LUG_LEFT, LUG_R, LUG_FILLET_LEFT, True)
ll_out, llm_out, lc_out = fillet_lc(L_lowleft, LUG_LEFT, LUG_R, LUG_FILLET_LEFT, False)
left_arc_mid = circle_arc_mid(LUG_LEFT, LUG_R, lc_in, lc_out)

wp = (
    cq.Workplane("XY")
    .moveTo(*bl2)
    .lineTo(*bt1)
    .threePointArc(btm, bt2)
    .lineTo(*v1)
    .threePointArc(vm, v2)
    .lineTo(*r1)
    .threePointArc(rm, r2)
    .lineTo(*tl_in)
    .threePointArc(tm_in, tc_in)
    .threePointArc(top_arc_mid, tp_top)
    .lineTo(*u1)
    .threePointArc(um, u2)
    .lineTo(*ll_in)
    .threePointArc(llm_in, lc_in)
    .threePointArc(left_arc_mid, lc_out)
    .threePointArc(llm_out, ll_out)
    .lineTo(*bl1)
    .threePointArc(blm, bl2)
    .close()
)
plate = wp.extrude(T)

# ---------------------------------------------------------------------------
# holes
# ---------------------------------------------------------------------------
# lug holes: counterbored from top
plate = (
    plate.faces(">Z").workplane(origin=(0, 0, T))
    .pushPoints([LUG_TOP, LUG_LEFT])
    .cboreHole(LUG_HOLE_D, LUG_CB_D, LUG_CB_DEPTH)
)
# top-counterbored hole
plate = (
    plate.faces(">Z").workplane(origin=(0, 0, T))
    .pushPoints([HOLE_TOP_CB])
    .cboreHole(TOP_HOLE_D, TOP_CB_D, TOP_CB_DEPTH)
)
# plain holes counterbored from the bottom
bottom_pts = [(x, -y) for (x, y) in HOLES]  # bottom workplane has mirrored Y
plate = (
    plate.faces("<Z").workplane(origin=(0, 0, 0))
    .pushPoints(bottom_pts)
    .cboreHole(HOLE_D, HOLE_CB_D, HOLE_CB_DEPTH)
)

# ---------------------------------------------------------------------------
# notch in right edge (open to the bottom)
# ---------------------------------------------------------------------------
d_r = v_norm(RIGHT_DIR)
n_out = right_n(d_r)
s0 = (NOTCH_Y0 - RIGHT_PT[1]) / d_r[1]
s1 = (NOTCH_Y1 - RIGHT_PT[1]) / d_r[1]
e0 = v_add(RIGHT_PT, v_mul(d_r, s0))
e1 = v_add(RIGHT_PT, v_mul(d_r, s1))
ext = 5.0
notch_pts = [
    v_add(e0, v_mul(n_out, ext)),
    v_add(e1, v_mul(n_out, ext)),
    v_sub(e1, v_mul(n_out, NOTCH_DEPTH)),
    v_sub(e0, v_mul(n_out, NOTCH_DEPTH)),
]
notch = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .polyline(notch_pts).close()
    .extrude(NOTCH_H + 1.0)
)
plate = plate.cut(notch)

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
